import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
L = 450.0          # overall length (X)
W = 288.0          # width over the side walls (Y)
H = 164.0          # height to top of lid (Z)
T = 2.5            # sheet thickness
SLOPE_X = -81.0    # x where the sloped nose starts at the top
END_H = 84.0       # height of the vertical -X end wall
LEDGE = 9.0        # flat ledge between the slope and the -X end wall
R_END = 8.0        # bend radius of the wrap-around -X end panel
PLATE_W = 300.0    # lid width (overhangs the side walls)
LIP = 8.0          # lid down-turned lip
RECESS = 4.0       # +X end panel recess behind the side-wall flanges
FLANGE = 8.0       # width of side-wall corner flanges at +X
TE = 6.0           # +X end panel (double skin) thickness

X0, X1 = -L / 2.0, L / 2.0

# lid boss
BOSS_X = -22.0
BOSS_D1, BOSS_H1 = 74.0, 17.5
BOSS_D2, BOSS_H2 = 68.0, 7.5
VENT_X, VENT_D = 23.5, 15.0

# side wall long slots (x_start, x_end, z) - extreme ends, both side walls
SLOT_W = 7.0
FRONT_SLOTS = [(-88.0, 184.5, 114.0), (-128.0, 184.5, 93.0),
               (-168.0, 184.5, 71.0), (-119.0, 134.0, 50.0)]
# back wall: shallow recessed panel above the top slot
WIN_X0, WIN_X1, WIN_Z0, WIN_Z1 = -79.0, 184.0, 120.0, 154.0

# +X end chevron pattern (for the -Y half, mirrored to +Y)
CHEV_W = 7.0
CHEV_SLOTS = [((-104.0, 136.0), (-20.0, 88.0)),
              ((-104.0, 117.0), (-20.0, 68.5)),
              ((-104.0, 97.5), (-20.0, 48.5)),
              ((-104.0, 78.0), (-18.0, 29.5))]
TRI_UP = [(-77.0, 138.0), (-16.0, 138.0), (-16.0, 105.0)]
TRI_LO = [(-107.0, 61.0), (-47.0, 29.5), (-107.0, 29.5)]

# bottom pipes (drain fittings)
PIPE_X, PIPE_Y = -66.0, 87.0
LEG_R, LEG_D, LEG_L = 15.5, 6.0, 18.0
PFL_D, PFL_T = 40.0, 2.2
PCYL_D, PCYL_H = 27.0, 14.0

# side pins
PIN_X, PIN_Z, PIN_D, PIN_L = 172.0, 35.0, 7.0, 12.0


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def line_isect(p, d, q, e):
    """intersection of p + s d and q + u e (2D)"""
    den = d[0] * e[1] - d[1] * e[0]
    s = ((q[0] - p[0]) * e[1] - (q[1] - p[1]) * e[0]) / den
    return (p[0] + s * d[0], p[1] + s * d[1])


def xz_prism(pts, y0, y1):
    """prism from XZ polygon between y0 and y1"""
    wp = cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close()
    return wp.extrude(y1 - y0)  # XZ normal is -Y


def yz_prism(pts, x0, x1):
    wp = cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close()
    return wp.extrude(x1 - x0)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def rect_between(plane, origin, a, b, width, depth):
    """rectangular cut between end points a,b (local) of given width"""
    cx, cy = (a[0] + b[0]) / 2.0, (a[1] + b[1]) / 2.0
    ln = math.hypot(b[0] - a[0], b[1] - a[1])
    ang = math.degrees(math.atan2(b[1] - a[1], b[0] - a[0]))
    return (cq.Workplane(plane, origin=origin)
            .transformed(offset=(cx, cy, 0), rotate=(0, 0, ang))
            .rect(ln, width).extrude(depth / 2.0, both=True))


def slot_between(plane, origin, a, b, width, depth):
    """rounded slot through a wall between extreme end points a,b (local)"""
    cx, cy = (a[0] + b[0]) / 2.0, (a[1] + b[1]) / 2.0
    ln = math.hypot(b[0] - a[0], b[1] - a[1])
    ang = math.degrees(math.atan2(b[1] - a[1], b[0] - a[0]))
    return (cq.Workplane(plane, origin=origin).center(cx, cy)
            .slot2D(ln, width, ang).extrude(depth / 2.0, both=True))


# ---------------------------------------------------------------------------
# main hollow sheet-metal body
# ---------------------------------------------------------------------------
SLOPE_Z = H - 6.0                        # slope starts just under the lid edge
SLOPE_EX = X0 + LEDGE                    # slope ends on a small ledge
outer = [(X0, 0.0), (X1, 0.0), (X1, H), (SLOPE_X, H), (SLOPE_X, SLOPE_Z),
         (SLOPE_EX, END_H), (X0, END_H)]
sd = (SLOPE_EX - SLOPE_X, END_H - SLOPE_Z)
sl = math.hypot(*sd)
sn = (-sd[1] / sl, sd[0] / sl)           # inward normal of the slope
sp = (SLOPE_X + T * sn[0], SLOPE_Z + T * sn[1])
i_top = line_isect(sp, sd, (0.0, H - T), (1.0, 0.0))
i_mid = line_isect(sp, sd, (0.0, END_H - T), (1.0, 0.0))
inner = [(X0 + T, T), (X1 - T, T), (X1 - T, H - T), i_top, i_mid,
         (X0 + T, END_H - T)]

outer_s = xz_prism(outer, -W / 2, W / 2)
outer_s = (outer_s.edges("|Z")
           .edges(cq.selectors.BoxSelector((X0 - 1, -W, -1), (X0 + 1, W, END_H + 1)))
           .fillet(R_END))
inner_s = xz_prism(inner, -W / 2 + T, W / 2 - T)
inner_s = (inner_s.edges("|Z")
           .edges(cq.selectors.BoxSelector((X0 + T - 1, -W, -1),
                                           (X0 + T + 1, W, END_H + 1)))
           .fillet(R_END - T))
body = outer_s.cut(inner_s)

# recess the +X end panel behind the side-wall corner flanges
body = body.cut(box(X1 - RECESS - 0.01, X1 + 1, -W / 2 + FLANGE, W / 2 - FLANGE,
                    T, H - T))
xe = X1 - RECESS
body = body.union(box(xe - TE, xe, -W / 2 + T, W / 2 - T, T, H - T))

# ---------------------------------------------------------------------------
# lid with down-turned lips
# ---------------------------------------------------------------------------
lid = box(SLOPE_X, X1, -PLATE_W / 2, PLATE_W / 2, H - T, H)
lid = lid.union(box(SLOPE_X, X1, -PLATE_W / 2, -PLATE_W / 2 + T, H - LIP, H))
lid = lid.union(box(SLOPE_X, X1, PLATE_W / 2 - T, PLATE_W / 2, H - LIP, H))
lid = lid.union(box(X1 - T, X1, -PLATE_W / 2, PLATE_W / 2, H - LIP, H))
body = body.union(lid)

# ---------------------------------------------------------------------------
# tabs on the side walls along the slope
# ---------------------------------------------------------------------------
def slope_pt(x):
    t = (x - SLOPE_X) / (SLOPE_EX - SLOPE_X)
    return (SLOPE_X + t * (SLOPE_EX - SLOPE_X), SLOPE_Z + t * (END_H - SLOPE_Z))


on = (-sn[0], -sn[1])  # outward normal
TAB_H = 11.0
for xa, xb in [(-125.0, -172.0)]:
    pa, pb = slope_pt(xa), slope_pt(xb)
    # start slightly inside the wall so it fuses
    pa_in = (pa[0] + 3 * sn[0], pa[1] + 3 * sn[1])
    pb_in = (pb[0] + 3 * sn[0], pb[1] + 3 * sn[1])
    tab = [pa_in, pb_in,
           (pb[0] + TAB_H * on[0], pb[1] + TAB_H * on[1]),
           (pa[0] + TAB_H * on[0], pa[1] + TAB_H * on[1])]
    body = body.union(xz_prism(tab, -W / 2, -W / 2 + 7.0))
    body = body.union(xz_prism(tab, W / 2 - 7.0, W / 2))

# ---------------------------------------------------------------------------
# base tray flanges (outside the side walls)
# ---------------------------------------------------------------------------
FT = 1.5
base_fl = [(X0 + R_END, 0.0), (X1 - 1.0, 0.0), (X1 - 1.0, 35.0), (215.5, 34.7),
           (205.3, 42.5), (192.3, 32.2), (179.4, 39.8), (172.0, 44.0),
           (163.9, 42.5), (148.6, 30.0), (-130.0, 30.0),
           (-130.0, 41.0), (-152.0, 31.0), (-161.0, 40.0), (X0 + R_END, 58.0)]
for s in (-1, 1):
    if s < 0:
        body = body.union(xz_prism(base_fl, -W / 2 - FT, -W / 2))
    else:
        body = body.union(xz_prism(base_fl, W / 2, W / 2 + FT))

# side-wall tabs poking through the -X end panel
for s in (-1, 1):
    yc = s * (W / 2 - R_END - 4.0)
    for zc in (25.0, 56.0):
        body = body.union(box(X0 - 2.5, X0 + 1.0, yc - 1.5, yc + 1.5,
                              zc - 5.0, zc + 5.0))

# ---------------------------------------------------------------------------
# side wall slots / windows
# ---------------------------------------------------------------------------
cuts = []
for (xa, xb, z) in FRONT_SLOTS:
    cuts.append(slot_between("XZ", (0, -W / 2, 0), (xa, z), (xb, z), SLOT_W, 12))
for (xa, xb, z) in FRONT_SLOTS:
    cuts.append(slot_between("XZ", (0, W / 2, 0), (xa, z), (xb, z), SLOT_W, 12))
cuts.append(box(WIN_X0, WIN_X1, W / 2 - 6, W / 2 + 6, WIN_Z0, WIN_Z1))

# tab-and-slot joints on side walls near +X end (vertical, tab ends flush)
for s in (-1, 1):
    for (za, zb) in [(114.0, 138.0), (27.0, 53.0)]:
        y_in, y_out = s * (W / 2 - 1.0), s * (W / 2 + 5.0)
        cuts.append(box(212.0, 219.0, min(y_in, y_out), max(y_in, y_out), za, zb))

# ---------------------------------------------------------------------------
# +X end panel chevrons and triangles
# ---------------------------------------------------------------------------
for m in (1, -1):
    for (a, b) in CHEV_SLOTS:
        cuts.append(slot_between("YZ", (xe, 0, 0), (m * a[0], a[1]),
                                 (m * b[0], b[1]), CHEV_W, 2 * TE + 6))
    for tri in (TRI_UP, TRI_LO):
        pts = [(m * p[0], p[1]) for p in tri]
        cuts.append(yz_prism(pts, xe - TE - 2, xe + 6))
# small slot / holes on end panel
cuts.append(box(xe - 1.0, xe + 6, -86.0, -61.0, 6.0, 14.5))
cuts.append(box(xe - TE - 2, xe + 6, -3.5, 0.5, 131.0, 155.0))

# ---------------------------------------------------------------------------
# lid vent hole
# ---------------------------------------------------------------------------
cuts.append(cq.Workplane("XY", origin=(VENT_X, 0, H - 10))
            .circle(VENT_D / 2).extrude(20))

# ---------------------------------------------------------------------------
# bottom slots (transverse) and arc slot
# ---------------------------------------------------------------------------
# floor stiffening beads (pressed inwards, seen as shallow grooves from below)
BEAD_W, BEAD_D = 6.0, 1.5
for x in [-28.0, 1.0, 60.0, 89.0, 118.0]:
    cuts.append(slot_between("XY", (0, 0, 0), (x, -101.0), (x, -5.0), BEAD_W,
                             2 * BEAD_D))
for x in [-27.0, 30.0, 60.0, 89.0, 118.0, 147.0]:
    cuts.append(slot_between("XY", (0, 0, 0), (x, 9.0), (x, 105.0), BEAD_W,
                             2 * BEAD_D))

ARC_CX, ARC_R, ARC_W = -114.0, 70.0, 4.0
arc_outer = (cq.Workplane("XY", origin=(ARC_CX, 0, -5)).circle(ARC_R + ARC_W / 2)
             .circle(ARC_R - ARC_W / 2).extrude(10))
arc_keep = box(ARC_CX, ARC_CX + 100, -100, 100, -6, 6)
cuts.append(arc_outer.cut(arc_keep))

# tab-and-slot joints along the base flange (shallow outlines) and holes
for s in (-1, 1):
    yo = s * (W / 2 + FT)
    for x in (-100.0, 0.0, 100.0):
        cuts.append(box(x - 14.0, x + 14.0, yo - 1.0, yo + 1.0, 7.5, 15.5)
                    .translate((0, -s * 0.2, 0)))
    for (x, z) in ((-50.0, 11.5), (50.0, 11.5), (161.0, 11.5), (172.0, 48.0),
                   (172.0, 21.0), (215.5, 83.0), (-154.0, 49.0), (-191.0, 31.0)):
        cuts.append(cq.Workplane("XZ", origin=(x, 0, z)).circle(1.6)
                    .extrude(W / 2 + 10, both=True))
    # tab slot just under the slope tab
    pa = slope_pt(-135.0)
    pb = slope_pt(-160.0)
    cuts.append(rect_between("XZ", (0, s * W / 2, 0),
                             (pa[0] + 7 * sn[0], pa[1] + 7 * sn[1]),
                             (pb[0] + 7 * sn[0], pb[1] + 7 * sn[1]), 6.0, 1.6))
# end panel small hole
cuts.append(cq.Workplane("YZ", origin=(xe - TE - 2, -37.0, 11.0)).circle(1.6).extrude(12))
# floor hole at arc centre with a 4-screw pattern
cuts.append(cq.Workplane("XY", origin=(ARC_CX, 0, -5)).circle(12.0).extrude(10))
cuts.append(cq.Workplane("XY", origin=(ARC_CX, 0, -5))
            .polarArray(20.0, 45.0, 360.0, 4).circle(1.5).extrude(10))
# diagonal seam across the sloped nose panel
p1 = slope_pt(-156.0)
p2 = slope_pt(-212.0)
a3 = cq.Vector(p1[0], 150.0, p1[1])
b3 = cq.Vector(p2[0], -150.0, p2[1])
cuts.append(cq.Workplane("XY").add(
    cq.Solid.makeCylinder(0.45, (b3 - a3).Length, a3, (b3 - a3).normalized())))

# lid seams (shallow grooves) and tab outlines
def groove(p, q, z_top, width=0.8, depth=0.6):
    cx, cy = (p[0] + q[0]) / 2.0, (p[1] + q[1]) / 2.0
    ln = math.hypot(q[0] - p[0], q[1] - p[1])
    ang = math.degrees(math.atan2(q[1] - p[1], q[0] - p[0]))
    return (cq.Workplane("XY", origin=(0, 0, z_top - depth)).center(cx, cy)
            .rect(ln + width, width).extrude(depth + 1.0)
            .rotate((cx, cy, 0), (cx, cy, 1), ang))


SEAMS = [((VENT_X + 6.0, 2.5), (214.0, 2.5)), ((214.0, 2.5), (X1 + 1, 13.0)),
         ((48.0, PLATE_W / 2 + 1), (48.0, 23.0)), ((48.0, 23.0), (VENT_X + 5.0, 4.0))]
for p, q in SEAMS:
    cuts.append(groove(p, q, H))
for sy in (-1, 1):
    cuts.append(box(62.0, 90.0, sy * 139.0 - 3.0, sy * 139.0 + 3.0, H - 0.6, H + 1))

for c in cuts:
    body = body.cut(c)

# trapezoidal stiffener outline on the lid near the +X end, end-panel tabs
def outline(pts, z_top):
    out = None
    for i in range(len(pts)):
        g = groove(pts[i], pts[(i + 1) % len(pts)], z_top)
        out = g if out is None else out.union(g)
    return out


body = body.cut(outline([(148.5, -42.5), (210.6, -59.6), (210.6, -90.6),
                         (148.5, -111.3)], H))
body = body.cut(box(211.0, 217.0, -86.0, -64.0, H - 0.6, H + 1))
body = body.cut(box(211.0, 217.0, 61.0, 86.0, H - 0.6, H + 1))
# small locating tab outline peeking out from under the boss
body = body.cut(outline([(-64.0, 6.0), (-64.0, -40.0), (-30.0, -17.0)], H))

# strips lying on the slope along both side walls (side wall in-turned flanges)
STRIP = 7.0
sa, sb = slope_pt(SLOPE_X), slope_pt(SLOPE_EX)
so = (sa[0] + T * on[0], sa[1] + T * on[1])
strip = [sa, sb, line_isect(so, sd, (SLOPE_EX, 0.0), (0.0, 1.0)),
         line_isect(so, sd, (SLOPE_X, 0.0), (0.0, 1.0))]
body = body.union(xz_prism(strip, -W / 2, -W / 2 + STRIP))
body = body.union(xz_prism(strip, W / 2 - STRIP, W / 2))

# recessed pocket behind the back-wall window
PK = 3.5
pocket = box(WIN_X0 - T, WIN_X1 + T, W / 2 - PK - T, W / 2 - T + 0.01,
             WIN_Z0 - T, WIN_Z1 + T)
pocket = pocket.cut(box(WIN_X0, WIN_X1, W / 2 - PK, W / 2 + 1, WIN_Z0, WIN_Z1))
body = body.union(pocket)

# ---------------------------------------------------------------------------
# internal shelf with tabs poking out through the +X end panel
# ---------------------------------------------------------------------------
SHELF_Z, SHELF_X0 = 80.0, -120.0
body = body.union(box(SHELF_X0, xe - TE + 0.01, -W / 2 + T - 0.01, W / 2 - T + 0.01,
                      SHELF_Z, SHELF_Z + T))
for m in (-1, 1):
    body = body.union(box(xe - TE - 0.01, xe + 3.5, min(m * 111.0, m * 135.0),
                          max(m * 111.0, m * 135.0), SHELF_Z, SHELF_Z + T))

# ---------------------------------------------------------------------------
# lid boss
# ---------------------------------------------------------------------------
boss = (cq.Workplane("XY", origin=(BOSS_X, 0, H - 1)).circle(BOSS_D1 / 2)
        .extrude(BOSS_H1 + 1)
        .faces(">Z").workplane().circle(BOSS_D2 / 2).extrude(BOSS_H2))
# seam across the boss cap
boss = boss.cut(groove((-46.0, 24.0), (12.0, 12.0), H + BOSS_H1 + BOSS_H2,
                       width=0.8, depth=0.6))
body = body.union(boss)


# ---------------------------------------------------------------------------
# drain fittings under the floor
# ---------------------------------------------------------------------------
for s in (-1, 1):
    py = s * PIPE_Y
    for k in range(3):
        a = math.radians(120.0 * k)
        lx, ly = PIPE_X + LEG_R * math.cos(a), py + LEG_R * math.sin(a)
        body = body.union(cq.Workplane("XY", origin=(lx, ly, -LEG_L))
                          .circle(LEG_D / 2).extrude(LEG_L + 1))
    body = body.union(cq.Workplane("XY", origin=(PIPE_X, py, -LEG_L - PFL_T))
                      .circle(PFL_D / 2).extrude(PFL_T))
    body = body.union(cq.Workplane("XY", origin=(PIPE_X, py, -LEG_L - PFL_T - PCYL_H))
                      .circle(PCYL_D / 2).extrude(PCYL_H))

# ---------------------------------------------------------------------------
# side pins
# ---------------------------------------------------------------------------
for s in (-1, 1):
    y0 = s * (W / 2 - 1.0)
    pin = (cq.Workplane("XZ", origin=(PIN_X, y0, PIN_Z)).circle(PIN_D / 2)
           .extrude(-s * PIN_L))
    body = body.union(pin)

result = body
